"""Knurled thumb screw: 18-lobe fluted head with an engraved serif "L" on its
front face, M8-style right-hand threaded shank ending in a truncated cone point.
Axis along Y: head at -Y (front face towards the viewer), shank towards +Y."""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
HEAD_D = 13.5            # knurled head diameter (over the lobes)
HEAD_L = 9.5             # head length along the axis
N_LOBES = 18             # number of knurl lobes
GROOVE_R = 0.60          # radius of each knurl groove
GROOVE_DEPTH = 0.68      # depth of knurl groove below the lobe tips
LOBE_FILLET = 0.42       # rounding of the lobe flanks (2D)
FRONT_FILLET = 0.38      # rounding of the front face outline
BACK_FILLET = 0.30       # rounding of the back face outline

THREAD_D = 8.0           # major diameter (M8)
THREAD_MINOR_D = 6.55    # minor diameter
PITCH = 1.2              # thread pitch (right-hand helical thread)
THREAD_L = 10.35         # threaded length from the head face
CONE_L = 2.0             # length of the cone point
TIP_D = 1.6              # diameter of the flat at the tip

ENGRAVE_DEPTH = 0.50     # depth of the engraved "L"

R = HEAD_D / 2.0

# ---------------- head: 18-lobe knurled profile ----------------
# Head axis is the Y axis; front face looks towards -Y, shaft goes towards +Y.
groove_c = R - GROOVE_DEPTH + GROOVE_R          # radius of groove centres
profile = cq.Sketch().circle(R)
for i in range(N_LOBES):
    a = math.radians(360.0 / N_LOBES * (i + 0.5))   # valleys between lobes (lobe at +X)
    profile = profile.push([(groove_c * math.cos(a), groove_c * math.sin(a))]).circle(GROOVE_R, mode="s").reset()
profile = profile.reset().vertices().fillet(LOBE_FILLET)

# XZ workplane: local x = +X, local y = +Z, normal = -Y
head = cq.Workplane("XZ").placeSketch(profile).extrude(HEAD_L)
head = head.faces("<Y").edges().fillet(FRONT_FILLET)
head = head.faces(">Y").edges().fillet(BACK_FILLET)

# ---------------- threaded shaft with cone point ----------------
# The shaft is built along +Z and then turned so that it runs along +Y.
r_maj = THREAD_D / 2.0
r_min = THREAD_MINOR_D / 2.0
r_tip = TIP_D / 2.0
r_in = r_min - 0.05                      # tooth root buried slightly in the core
HW_ROOT = 0.45 * PITCH                   # half width of the tooth at the root
HW_CREST = 0.06 * PITCH                  # half width of the crest flat
T_START = -1.39                          # tooth starts inside the head (sets thread phase)
T_LEN = THREAD_L - T_START + 1.5         # and runs past the cone start (clipped)

def _helix(r, dz):
    return cq.Wire.makeHelix(PITCH, T_LEN, r, center=cq.Vector(0, 0, T_START + dz))

_h = [_helix(r_in, -HW_ROOT), _helix(r_maj, -HW_CREST),
      _helix(r_maj, HW_CREST), _helix(r_in, HW_ROOT)]
_faces = [cq.Face.makeRuledSurface(_h[i], _h[(i + 1) % 4]) for i in range(4)]
for _end in (False, True):
    _pts = [w.endPoint() if _end else w.startPoint() for w in _h]
    _faces.append(cq.Face.makeFromWires(cq.Wire.makePolygon(_pts, close=True)))
tooth = cq.Solid.makeSolid(cq.Shell.makeShell(_faces))
tooth = cq.Workplane("XY").add(tooth).intersect(
    cq.Workplane("XY").workplane(offset=T_START - 1).circle(r_maj + 1).extrude(THREAD_L - T_START + 1)
)

core = (
    cq.Workplane("XZ")
    .polyline([(0, -0.5), (r_min, -0.5), (r_min, THREAD_L),
               (r_tip, THREAD_L + CONE_L), (0, THREAD_L + CONE_L)])
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)
shaft = core.union(tooth).rotate((0, 0, 0), (1, 0, 0), -90)

part = head.union(shaft)

# ---------------- engraved "L" on the front face ----------------
def P(x, z):
    return (x * R, z * R)

L_sketch = (
    cq.Workplane("XZ", origin=(0, -HEAD_L, 0))
    .moveTo(*P(-0.406, -0.428))
    .lineTo(*P(0.427, -0.428))
    .lineTo(*P(0.460, -0.127))
    .threePointArc(P(0.250, -0.340), P(0.0, -0.390))
    .threePointArc(P(-0.080, -0.368), P(-0.106, -0.300))
    .lineTo(*P(-0.106, 0.410))
    .threePointArc(P(-0.066, 0.476), P(0.054, 0.514))
    .lineTo(*P(0.060, 0.536))
    .lineTo(*P(-0.406, 0.536))
    .lineTo(*P(-0.404, 0.516))
    .threePointArc(P(-0.297, 0.485), P(-0.242, 0.410))
    .lineTo(*P(-0.242, -0.292))
    .threePointArc(P(-0.266, -0.370), P(-0.404, -0.408))
    .close()
)
L_cut = L_sketch.extrude(-ENGRAVE_DEPTH)   # into the head (towards +Y)
part = part.cut(L_cut)

result = part
VIEW = {"azimuth": 45, "elevation": 26}
